import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Robot arm on a round base housing.
# The base flange faces -Y, the arm runs along +Y.  The arm (shoulder saddle,
# upper arm, forearm, wrist plate and gripper) is built in its own frame with
# vertical joint axes and then rolled about the housing axis (Y) by ARM_ROLL.
# ---------------------------------------------------------------------------

# --- base -------------------------------------------------------------------
FL_D = 100.0          # flange diameter
FL_T = 4.0            # flange thickness
BODY_D = 80.0         # housing diameter
BODY_END = 47.0       # housing back face (Y)
CAP_D = 76.0          # small rim at the back
CAP_END = 50.0
POCKET_D = 74.0       # front recess diameter
POCKET_DEPTH = 30.0
V_ANG = 50.8          # angle where the notch meets the recess circle
V_X = 9.5             # notch inner vertical edge (X)
V_Z = 10.5
FL_HOLE_OFF = 32.0    # flange bolt holes at (+-off, +-off)
FL_HOLE_D = 3.0
BLK_ANG = 35.0        # block standing in the recess, turned about Z

# --- arm (local frame, before the roll) -------------------------------------
ARM_ROLL = -12.8      # roll of the whole arm about the housing axis (top to -X)
AX = 12.7             # X of all vertical joint axes
SH_Y = 80.0           # shoulder axis
EL_Y = 182.0          # elbow axis
WR_Y = 290.0          # wrist axis
JZ = -2.7             # underside of the upper arm / top of the shoulder saddle
FA_Z1 = -1.8          # top of the forearm
SAD_Z0 = -18.0        # underside of the shoulder saddle
SAD_R = 20.0          # round end of the saddle around the shoulder axis
UA_Z1 = 12.3          # crown of the upper arm
UA_END_Z = 7.5        # top of the upper arm at its two extreme ends
UA_R_SH = 17.5        # upper arm end radius at the shoulder
UA_R_EL = 18.0        # upper arm end radius at the elbow
UA_FILLET = 6.0
UA_WALL = 2.6         # wall left around the end bores
FA_R = 15.5           # forearm half width
FA_Z0 = -19.8         # forearm underside
FA_HOOD_Z = 2.0       # raised housing around the side window
FA_LOBE_Z = -21.8     # cups below the forearm
WP_Z1 = 3.0           # wrist plate top
WP_R = 12.5
GR_Y = 322.5          # gear axis Y
GR_ZC = 7.4           # gripper symmetry plane height
GEAR_PITCH = 11.5     # gear pitch radius


def ycyl(d, y0, y1, x=0.0, z=0.0):
    """cylinder along +Y from y0 to y1"""
    return (cq.Workplane("XZ", origin=(0, y0, 0)).center(x, z)
            .circle(d / 2.0).extrude(-(y1 - y0)))


def zcyl(d, z0, z1, x=0.0, y=0.0):
    return (cq.Workplane("XY", origin=(0, 0, z0)).center(x, y)
            .circle(d / 2.0).extrude(z1 - z0))


def xcyl(d, x0, x1, y=0.0, z=0.0):
    return (cq.Workplane("YZ", origin=(x0, 0, 0)).center(y, z)
            .circle(d / 2.0).extrude(x1 - x0))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def yz_poly(pts, x0, x1):
    return cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close().extrude(x1 - x0)


def slot_xy(p0, p1, w, z0, z1):
    """stadium between two points in XY, extruded in Z"""
    (x0, y0), (x1, y1) = p0, p1
    L = math.hypot(x1 - x0, y1 - y0)
    ang = math.degrees(math.atan2(y1 - y0, x1 - x0))
    s = (cq.Workplane("XY", origin=(0, 0, z0)).slot2D(L + w, w, 0).extrude(z1 - z0))
    return s.rotate((0, 0, 0), (0, 0, 1), ang).translate(((x0 + x1) / 2, (y0 + y1) / 2, 0))


def slot_yz(p0, p1, w, x0, x1):
    """stadium between two points in YZ, extruded along X"""
    (ya, za), (yb, zb) = p0, p1
    L = math.hypot(yb - ya, zb - za)
    ang = math.degrees(math.atan2(zb - za, yb - ya))
    s = cq.Workplane("YZ", origin=(x0, 0, 0)).slot2D(L + w, w, 0).extrude(x1 - x0)
    return s.rotate((0, 0, 0), (1, 0, 0), ang).translate((0, (ya + yb) / 2, (za + zb) / 2))


# ===========================================================================
# BASE HOUSING
# ===========================================================================
base = ycyl(FL_D, 0, FL_T)
base = base.union(ycyl(BODY_D, FL_T - 0.5, BODY_END))
base = base.union(ycyl(CAP_D, BODY_END - 0.5, CAP_END))

# front recess: circle minus a V shaped land on the +X side
R_P = POCKET_D / 2.0
vx = R_P * math.cos(math.radians(V_ANG))
vz = R_P * math.sin(math.radians(V_ANG))
pocket = (cq.Workplane("XZ", origin=(0, -1, 0))
          .moveTo(vx, vz).lineTo(V_X, V_Z).lineTo(V_X, -V_Z).lineTo(vx, -vz)
          .threePointArc((-R_P, 0), (vx, vz)).close()
          .extrude(-(POCKET_DEPTH + 1)))
base = base.cut(pocket)

# lens shaped window in the land
lens = (cq.Workplane("XZ", origin=(0, -1, 0))
        .moveTo(20.0, 14.7).lineTo(24.2, 18.5)
        .threePointArc((30.5, 0), (24.2, -18.5))
        .lineTo(20.0, -14.7).close()
        .extrude(-11.0))
base = base.cut(lens)

# block standing in the recess (turned about Z, trimmed by the recess wall)
blk = box(-14.0, 0.0, 0.0, 14.0, -11.0, 11.0).rotate((0, 0, 0), (0, 0, 1), BLK_ANG)
blk = blk.translate((-26.3, 22.0, 0))   # front right corner of the block
blk = blk.intersect(ycyl(POCKET_D + 0.2, 1.0, POCKET_DEPTH + 0.5))
base = base.union(blk)

# centre holes in the recess floor
base = base.cut(ycyl(6.0, POCKET_DEPTH - 1, POCKET_DEPTH + 8))
for sx, sz in ((-5.8, -1.2), (5.8, 1.2)):
    base = base.cut(ycyl(2.5, POCKET_DEPTH - 1, POCKET_DEPTH + 5, sx, sz))

# flange bolt holes
for sx in (-1, 1):
    for sz in (-1, 1):
        base = base.cut(ycyl(FL_HOLE_D, -1, FL_T + 1, sx * FL_HOLE_OFF, sz * FL_HOLE_OFF))

# small port boss on the +X side of the housing
base = base.union(xcyl(7.0, BODY_D / 2 - 3, BODY_D / 2 + 1.5, 12.0, 0.0))
base = base.cut(xcyl(3.5, BODY_D / 2 - 6, BODY_D / 2 + 2, 12.0, 0.0))

# a square lug and a round boss on the back face
LUG_Z = 3.5
lug = box(-25.5, -17.5, CAP_END - 1, CAP_END + 10, LUG_Z - 4.0, LUG_Z + 4.0)
lug = lug.cut(ycyl(3.5, CAP_END + 3, CAP_END + 11, -21.5, LUG_Z))
base = base.union(lug)
lug = ycyl(6.5, CAP_END - 1, CAP_END + 13, -3.5, LUG_Z)
lug = lug.cut(ycyl(2.5, CAP_END + 4, CAP_END + 14, -3.5, LUG_Z))
base = base.union(lug)

# ===========================================================================
# SHOULDER SADDLE (arm frame)
# ===========================================================================
SAD_XL, SAD_XR = -31.0, 24.0        # saddle width where it meets the housing
SAD_YL = 61.0                       # end of its straight left edge


def saddle_plan(z0, z1, inset=0.0):
    r = SAD_R - inset
    xl, xr = SAD_XL + inset, SAD_XR - inset
    yr = SH_Y - math.sqrt(max(r ** 2 - (xr - AX) ** 2, 0.0))
    dx, dy = xl - AX, SAD_YL - SH_Y
    a = math.atan2(dy, dx) - math.acos(r / math.hypot(dx, dy))
    tl = (AX + r * math.cos(a), SH_Y + r * math.sin(a))
    am = math.radians(70)
    return (cq.Workplane("XY", origin=(0, 0, z0))
            .moveTo(xl, CAP_END - 2)
            .lineTo(xr, CAP_END - 2)
            .lineTo(xr, yr)
            .threePointArc((AX + r * math.cos(am), SH_Y + r * math.sin(am)), tl)
            .lineTo(xl, SAD_YL)
            .close()
            .extrude(z1 - z0))


saddle = saddle_plan(SAD_Z0, JZ)
saddle = saddle.edges("|Z").fillet(7.0)
saddle = saddle.faces(">Z").edges().fillet(1.5)
# hollow underside (cup) of the saddle
saddle = saddle.cut(saddle_plan(SAD_Z0 - 1, SAD_Z0 + 5.0, inset=4.0))

# ===========================================================================
# UPPER ARM (arm frame)
# ===========================================================================
ua_plan = (cq.Workplane("XY", origin=(0, 0, JZ))
           .moveTo(AX - UA_R_SH, SH_Y)
           .threePointArc((AX, SH_Y - UA_R_SH), (AX + UA_R_SH, SH_Y))
           .lineTo(AX + 13, SH_Y + 32)
           .lineTo(AX + 14, EL_Y - 30)
           .lineTo(AX + UA_R_EL, EL_Y)
           .threePointArc((AX, EL_Y + UA_R_EL), (AX - UA_R_EL, EL_Y))
           .lineTo(AX - 12.5, EL_Y - 30)
           .lineTo(AX - 12.5, SH_Y + 32)
           .close()
           .extrude(UA_Z1 - JZ))
ua_plan = ua_plan.faces(">Z").edges().fillet(UA_FILLET)
# side profile: crowned, dropping towards both ends
ua_side = (cq.Workplane("YZ", origin=(AX - 30, 0, 0))
           .moveTo(SH_Y - 20, JZ - 1)
           .lineTo(SH_Y - 20, UA_END_Z)
           .threePointArc((SH_Y - 4, UA_Z1 - 1.6), (SH_Y + 15, UA_Z1))
           .lineTo(EL_Y - 15, UA_Z1)
           .threePointArc((EL_Y + 4, UA_Z1 - 1.6), (EL_Y + 20, UA_END_Z))
           .lineTo(EL_Y + 20, JZ - 1)
           .close()
           .extrude(60))
upper_arm = ua_plan.intersect(ua_side)
# open bores at both ends
upper_arm = upper_arm.cut(zcyl(2 * (UA_R_SH - UA_WALL), JZ + 2, UA_Z1 + 2, AX, SH_Y))
upper_arm = upper_arm.cut(zcyl(2 * (UA_R_EL - UA_WALL), JZ + 2, UA_Z1 + 2, AX, EL_Y))
# cable passage from each bore into the beam
CBL_Z = JZ + 8.0
upper_arm = upper_arm.cut(ycyl(6.5, SH_Y, SH_Y + UA_R_SH + 8, AX, CBL_Z))
upper_arm = upper_arm.cut(ycyl(6.5, EL_Y - UA_R_EL - 8, EL_Y, AX, CBL_Z))
# pivot pins in the bores
for py in (SH_Y, EL_Y):
    upper_arm = upper_arm.union(zcyl(6.0, JZ, JZ + 5, AX, py))
    upper_arm = upper_arm.cut(zcyl(2.0, JZ, JZ + 6, AX, py))

# ===========================================================================
# FOREARM (arm frame)
# ===========================================================================
forearm = slot_xy((AX, EL_Y), (AX, WR_Y - 4), 2 * FA_R, FA_Z0, FA_Z1)
# raised housing around the side window, rounded at both ends
hood = box(AX - FA_R, AX + FA_R, 214.5, 256.5, FA_Z1 - 4.0, FA_HOOD_Z)
hood = hood.edges("|Z").fillet(4.0).faces(">Z").edges().fillet(2.0)
forearm = forearm.union(hood)
# side window right through
WIN_Y0, WIN_Y1, WIN_Z0, WIN_Z1 = 223.0, 251.0, -14.0, -3.0
WIN_ZC = 0.5 * (WIN_Z0 + WIN_Z1)
forearm = forearm.cut(box(AX - 25, AX + 25, WIN_Y0, WIN_Y1, WIN_Z0, WIN_Z1))
# T-shaped slots either side of the window
for yy, sgn in ((WIN_Y0, -1), (WIN_Y1, 1)):
    forearm = forearm.cut(box(AX + FA_R - 3.5, AX + 25, min(yy, yy + sgn * 12), max(yy, yy + sgn * 12),
                              WIN_ZC - 0.9, WIN_ZC + 0.9))
    forearm = forearm.cut(box(AX + FA_R - 3.5, AX + 25, min(yy + sgn * 3, yy + sgn * 4.5),
                              max(yy + sgn * 3, yy + sgn * 4.5), WIN_Z0 + 1.2, WIN_Z1 - 1.2))
# cups on the underside at both joints
for y0, y1 in ((162.5, 207.0), (243.0, 298.5)):
    w = 26.0
    cup = slot_xy((AX, y0 + w / 2), (AX, y1 - w / 2), w, FA_LOBE_Z, FA_Z0 + 3.0)
    cup = cup.faces("<Z").edges().chamfer(1.8)
    forearm = forearm.union(cup)
    forearm = forearm.cut(slot_xy((AX, y0 + w / 2), (AX, y1 - w / 2), w - 6, FA_LOBE_Z - 1, FA_LOBE_Z + 5))
    forearm = forearm.union(box(AX - 6.5, AX + 6.5, (y0 + y1) / 2 - 7, (y0 + y1) / 2 + 7,
                                FA_LOBE_Z + 2.5, FA_LOBE_Z + 6))

# ===========================================================================
# WRIST PLATE (arm frame)
# ===========================================================================
wrist = (cq.Workplane("XY", origin=(0, 0, FA_Z1))
         .moveTo(AX + WP_R, WR_Y)
         .threePointArc((AX, WR_Y - WP_R), (AX - WP_R, WR_Y))
         .lineTo(AX - WP_R, WR_Y + 9)
         .lineTo(AX - 3, WR_Y + 22)
         .lineTo(AX + 6, WR_Y + 24)
         .lineTo(AX + WP_R, WR_Y + 14)
         .close()
         .extrude(WP_Z1 - FA_Z1))
wrist = wrist.cut(zcyl(3.0, FA_Z1 - 1, WP_Z1 + 1, AX, WR_Y))

# ===========================================================================
# GRIPPER (arm frame): carrier plate, two meshing sector gears with finger
# arms, two outer parallel links and two hooked fingers
# ===========================================================================
FX0, FX1 = 10.5, 18.5           # fingers (set back behind the linkage)
CAR_X0, CAR_X1 = 20.0, 23.5     # gear carrier plate
GEAR_X0, GEAR_X1 = 23.5, 27.5   # gears with their finger arms
LNK_X0, LNK_X1 = 27.5, 30.0     # outer parallel links


def gz(dz):
    return GR_ZC + dz


# carrier plate rising from the wrist plate behind the gears
carrier = (cq.Workplane("YZ", origin=(CAR_X0, 0, 0))
           .moveTo(WR_Y + 12, FA_Z1)
           .lineTo(WR_Y + 30, FA_Z1)
           .lineTo(WR_Y + 36, gz(-15.0))
           .lineTo(WR_Y + 46, gz(-15.0))
           .lineTo(WR_Y + 55, gz(-5.0))
           .lineTo(WR_Y + 55, gz(5.0))
           .lineTo(WR_Y + 46, gz(17.0))
           .lineTo(WR_Y + 38, gz(24.0))
           .lineTo(WR_Y + 27, gz(24.0))
           .spline([(WR_Y + 22, gz(15.0)), (WR_Y + 19, gz(10.0)), (WR_Y + 16, gz(6.0)),
                    (WR_Y + 14, WP_Z1 + 1.0), (WR_Y + 12, FA_Z1)], includeCurrent=True)
           .close()
           .extrude(CAR_X1 - CAR_X0))
gripper = carrier
# thick top knuckle of the carrier reaching back over the fingers
gripper = gripper.union(box(FX0 + 0.5, CAR_X1, WR_Y + 24, WR_Y + 35, gz(16.0), gz(23.0))
                        .edges("|X").fillet(2.5))


def gear(cy, cz, face_dir, x0, x1, arm_to, n=16, half_sector=75.0):
    """sector gear (teeth on the side facing face_dir) with an arm to a finger pivot"""
    rp = GEAR_PITCH
    ro, ri = rp + 1.25, rp - 1.25
    da = 2 * math.pi / n
    g = xcyl(2 * (rp - 0.4), x0, x1, cy, cz)
    for i in range(n):
        a0 = da * i
        mid = a0 + 0.5 * da
        d = math.degrees(math.atan2(math.sin(mid - face_dir), math.cos(mid - face_dir)))
        if abs(d) < half_sector:
            pts = []
            for f, r in ((0.0, ri), (0.2, ro), (0.48, ro), (0.68, ri)):
                a = a0 + f * da
                pts.append((cy + r * math.cos(a), cz + r * math.sin(a)))
            g = g.union(yz_poly(pts, x0, x1))
    g = g.union(slot_yz((cy, cz), arm_to, 7.0, x0, x1))
    g = g.cut(xcyl(2.2, x0 - 1, x1 + 1, cy, cz))
    for k in range(3):
        a = math.radians(90 + 120 * k)
        g = g.cut(xcyl(1.2, x0 - 1, x1 + 1, cy + 3.5 * math.cos(a), cz + 3.5 * math.sin(a)))
    return g


# finger outline (Y, height above the gripper plane) for the upper finger
FINGER = [(336.0, 27.6), (340.0, 31.3), (348.0, 29.0), (361.0, 23.8), (371.0, 24.1),
          (385.0, 21.9), (391.0, 17.7), (392.0, 13.9), (388.5, 11.5), (382.0, 14.3),
          (371.0, 16.9), (363.0, 14.8), (356.0, 14.0), (348.0, 18.6), (341.0, 23.3)]
P_A = (342.0, 27.2)     # finger pivot on the gear arm
P_B0 = (340.0, 2.6)     # outer link pivot on the carrier
P_B1 = (360.8, 17.3)    # outer link pivot on the finger


def finger_set(sign):
    def pt(p):
        return (p[0], gz(sign * p[1]))
    g_c = (GR_Y, gz(sign * GEAR_PITCH))
    p_a, p_b0, p_b1 = pt(P_A), pt(P_B0), pt(P_B1)
    s = gear(g_c[0], g_c[1], math.radians(-60 * sign), GEAR_X0, GEAR_X1, p_a)
    s = s.union(slot_yz(p_b0, p_b1, 5.5, LNK_X0, LNK_X1))
    f_pts = [pt(p) for p in FINGER]
    s = s.union(cq.Workplane("YZ", origin=(FX0, 0, 0)).spline(f_pts, periodic=True).close()
                .extrude(FX1 - FX0))
    # knuckle spacers between finger, gear arm and links, with pin heads
    s = s.union(xcyl(6.5, FX1 - 0.5, GEAR_X0 + 0.5, p_a[0], p_a[1]))
    s = s.union(xcyl(6.0, FX1 - 0.5, LNK_X0 + 0.5, p_b1[0], p_b1[1]))
    s = s.union(xcyl(6.0, CAR_X1 - 0.5, LNK_X0 + 0.5, p_b0[0], p_b0[1]))
    for c in (p_a, p_b1, p_b0):
        s = s.union(xcyl(3.6, GEAR_X1 - 0.5, LNK_X1 + 0.8, c[0], c[1]))
    s = s.union(xcyl(3.6, CAR_X0 - 0.8, GEAR_X1 + 0.8, g_c[0], g_c[1]))
    return s


gripper = gripper.union(finger_set(1)).union(finger_set(-1))

# ===========================================================================
# ASSEMBLY: roll the arm about the housing axis and join it to the base
# ===========================================================================
arm = saddle.union(upper_arm).union(forearm).union(wrist).union(gripper)
arm = arm.rotate((0, 0, 0), (0, 1, 0), ARM_ROLL)
result = base.union(arm)

VIEW = {"azimuth": 45, "elevation": 26}
